import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
boss_r = 8.0            # outer radius of the three bosses
hole_d = 9.0            # through-hole diameter
y_spacing = 53.5        # distance between the two rear bosses (along Y)
x_reach = 100.6         # distance from rear boss centres to the tip boss (along X)
plate_t = 3.9           # plate thickness
rear_boss_h = 6.35      # total height of the two rear bosses (from plate bottom)
tip_boss_h = 10.45      # total height of the tip boss (from plate bottom)
side_arc_r = 150.0      # radius of the two convex side arcs

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- layout ----------------
x0 = -x_reach / 2.0                 # rear boss X
A = (x0, y_spacing / 2.0)           # rear boss (+Y)
B = (x0, -y_spacing / 2.0)          # rear boss (-Y)
C = (x0 + x_reach, 0.0)             # tip boss


def sub(p, q):
    return (p[0] - q[0], p[1] - q[1])


def add(p, q):
    return (p[0] + q[0], p[1] + q[1])


def mul(p, s):
    return (p[0] * s, p[1] * s)


def unit(p):
    n = math.hypot(p[0], p[1])
    return (p[0] / n, p[1] / n)


def mirror(p):
    return (p[0], -p[1])


# Centre of the upper side arc: on the perpendicular bisector of A-C such that
# the arc (radius side_arc_r) is tangent to both boss circles (bosses inside).
M = mul(add(A, C), 0.5)
d = sub(C, A)
L = math.hypot(d[0], d[1])
nrm = unit((d[1], -d[0]))            # pointing away from the upper edge
dist_c = side_arc_r - boss_r
h = math.sqrt(dist_c ** 2 - (L / 2.0) ** 2)
c_top = add(M, mul(nrm, h))

# tangent points of the upper arc on the boss circles
tA = add(A, mul(unit(sub(A, c_top)), boss_r))
tC = add(C, mul(unit(sub(C, c_top)), boss_r))
mid_dir = unit(add(unit(sub(tA, c_top)), unit(sub(tC, c_top))))
mTop = add(c_top, mul(mid_dir, side_arc_r))

tB = mirror(tA)
tCb = mirror(tC)
mBot = mirror(mTop)

# straight rear edge, tangent to both rear bosses
lA = (x0 - boss_r, A[1])
lB = (x0 - boss_r, B[1])

# Plate outline: the boss portions are routed through the boss centres so that
# the full-height boss cylinders form the rounded corners of the plate.
plate = (
    cq.Workplane("XY")
    .moveTo(*lB)
    .lineTo(*lA)
    .lineTo(*A)
    .lineTo(*tA)
    .threePointArc(mTop, tC)
    .lineTo(*C)
    .lineTo(*tCb)
    .threePointArc(mBot, tB)
    .lineTo(*B)
    .close()
    .extrude(plate_t)
)


def cylinder(center, radius, z0, height, seam_deg):
    """Vertical cylinder; its seam line is turned to seam_deg (degrees about Z)."""
    cyl = cq.Solid.makeCylinder(radius, height,
                                cq.Vector(center[0], center[1], z0),
                                cq.Vector(0, 0, 1))
    cyl = cyl.rotate(cq.Vector(center[0], center[1], 0),
                     cq.Vector(center[0], center[1], 1), seam_deg)
    return cq.Workplane("XY").add(cyl)


# seam positions chosen on the plate-covered side of each boss, facing away
# from the usual viewing directions
seam_A = 45.0
seam_B = 135.0
seam_C = 180.0
seam_hole = -45.0

body = (
    plate.union(cylinder(A, boss_r, 0.0, rear_boss_h, seam_A))
    .union(cylinder(B, boss_r, 0.0, rear_boss_h, seam_B))
    .union(cylinder(C, boss_r, 0.0, tip_boss_h, seam_C))
)

for p in (A, B, C):
    body = body.cut(cylinder(p, hole_d / 2.0, -1.0, tip_boss_h + 2.0, seam_hole))

result = body
